import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# wheel axis = Y ; shaft sticks out toward -Y (front)
R_TIRE = 100.0        # tyre outer radius (crown top)
R_SIDE = 90.4         # radius where flat tyre side meets the crown
W_TIRE = 53.6         # tyre width (between flat sides)

# front plate (shaft side)
T_PLATE = 5.3         # thickness
R_PLATE_IN = 66.0     # radius at tyre side
R_PLATE_OUT = 61.5    # radius at front face (conical edge)

# back hub
T_HUB = 15.5
R_HUB = 64.6
HUB_CH_R = 4.6        # chamfer radial
HUB_CH_A = 5.8        # chamfer axial

# back centre boss
R_BOSS = 25.7
T_BOSS = 3.7

# shaft
D_SHAFT = 18.4
L_SHAFT = 62.2
D_TIP = 9.3
L_TIP = 13.1
TIP_CH = 0.3
TIP_FILLET = 0.3     # fillet at root of tip pin
FLAT_DEPTH = 3.0
FLAT_GAP_WHEEL = 7.5  # plain length between plate and start of flat
FLAT_GAP_TIP = 3.2    # plain length between end of flat and shoulder

SEAM_ANG = 165.0      # angular position of the wheel revolve seam (cosmetic only)

# ---------------- derived axial positions ----------------
y_tf = -W_TIRE / 2.0              # tyre front side
y_tb = W_TIRE / 2.0               # tyre back side
y_pf = y_tf - T_PLATE             # front plate face
y_hb = y_tb + T_HUB               # hub back face
y_bb = y_hb + T_BOSS              # boss back face

# ---------------- wheel body (revolved profile) ----------------
# profile drawn in XY plane: x = radius, y = axial ; revolved about Y
prof = (
    cq.Workplane("XY")
    .moveTo(0, y_bb)
    .lineTo(R_BOSS, y_bb)
    .lineTo(R_BOSS, y_hb)
    .lineTo(R_HUB - HUB_CH_R, y_hb)
    .lineTo(R_HUB, y_hb - HUB_CH_A)
    .lineTo(R_HUB, y_tb)
    .lineTo(R_SIDE, y_tb)
    .threePointArc((R_TIRE, 0.0), (R_SIDE, y_tf))
    .lineTo(R_PLATE_IN, y_tf)
    .lineTo(R_PLATE_OUT, y_pf)
    .lineTo(0, y_pf)
    .close()
)
wheel = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 1, 0), SEAM_ANG)

# ---------------- shaft (revolved profile) ----------------
y_sh = y_pf - L_SHAFT               # shoulder (shaft -> tip pin)
y_te = y_sh - L_TIP                 # tip end
r_s = D_SHAFT / 2.0
r_t = D_TIP / 2.0
f = TIP_FILLET
c45 = 0.70710678
shaft_prof = (
    cq.Workplane("XY")
    .moveTo(0, y_pf + 1.0)                      # small overlap into the plate
    .lineTo(r_s, y_pf + 1.0)
    .lineTo(r_s, y_sh)
    .lineTo(r_t + f, y_sh)
    .threePointArc((r_t + f - f * c45, y_sh - f + f * c45), (r_t, y_sh - f))
    .lineTo(r_t, y_te + TIP_CH)
    .lineTo(r_t - TIP_CH, y_te)
    .lineTo(0, y_te)
    .close()
)
# revolve, then turn the seam to -X where it is out of sight
shaft = shaft_prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 1, 0), 180)

# flat on the underside (-Z) of the shaft
flat_len = L_SHAFT - FLAT_GAP_WHEEL - FLAT_GAP_TIP
flat_cut = (
    cq.Workplane("XY")
    .box(D_SHAFT * 2, flat_len, D_SHAFT)
    .translate((0, y_pf - FLAT_GAP_WHEEL - flat_len / 2.0,
                -D_SHAFT / 2.0 + FLAT_DEPTH - D_SHAFT / 2.0))
)
shaft = shaft.cut(flat_cut)

result = wheel.union(shaft)

VIEW = {"azimuth": 45, "elevation": 26}
